import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 100.0            # outer diameter of the knurled roller
L = 60.0             # axial length (axis = X)
R = D / 2.0

N_GROOVES = 10       # grooves per hand (left + right hand helices)
TWIST = 72.0         # rotation of each groove over the full length (deg)
G_R = 5.35           # groove profile radius (round bottom)
G_OFF = 0.5          # groove profile centre sits this far outside the OD
G_EXT = 1.0          # groove tools overrun the end faces by this much

BORE_D = 30.0        # through bore
CB_D = 52.6          # counterbore on +X face
CB_DEPTH = 30.0      # counterbore depth

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- body ----------------
x0 = -L / 2.0
SEAM_ANG = -50.0     # park the OD cylinder seam where it is seen edge-on
body = (
    cq.Workplane("YZ", origin=(x0, 0, 0))
    .circle(R)
    .extrude(L)
    .val()
    .rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), SEAM_ANG)
)


def groove(hand, i, dr=0.0):
    """One helical round-bottom groove (profile in the end plane, twisted
    about the part axis).  The profile circle is built on the +Y side of
    the YZ workplane (its seam then points radially outward, outside the
    material) and the finished tool is rotated into place about X."""
    rc = R + G_OFF + dr
    length = L + 2 * G_EXT
    tw = hand * TWIST * length / L
    g = (
        cq.Workplane("YZ", origin=(x0 - G_EXT, 0, 0))
        .moveTo(rc, 0)
        .circle(G_R)
        .twistExtrude(length, tw, combine=False)
        .val()
    )
    ang = 360.0 / N_GROOVES * i - hand * TWIST * G_EXT / L
    return g.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), ang)


def knurl(blank, fuzzy=True):
    b = blank
    for hand in (1, -1):
        for i in range(N_GROOVES):
            if fuzzy:
                # the two groove families touch tangentially at every
                # crossing point -> a small fuzzy value keeps OCCT happy
                b = b.cut(groove(hand, i), tol=0.01)
            else:
                # fallback: break the tangency by a hair instead
                b = b.cut(groove(hand, i, 0.05 if hand < 0 else 0.0))
    return b


blank = body
body = knurl(blank, fuzzy=True)
if not (body.isValid() and len(body.Solids()) == 1):
    body = knurl(blank, fuzzy=False)

# ---------------- bore + counterbore ----------------
bore = (
    cq.Workplane("YZ", origin=(x0 - 1, 0, 0))
    .circle(BORE_D / 2)
    .extrude(L + 2)
    .val()
)
cb = (
    cq.Workplane("YZ", origin=(L / 2.0 - CB_DEPTH, 0, 0))
    .circle(CB_D / 2)
    .extrude(CB_DEPTH + 1)
    .val()
    # turn the cylinder seam to the -Y side (out of sight in the usual views)
    .rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 180)
)
body = body.cut(bore).cut(cb)

result = cq.Workplane("XY").newObject([body.Solids()[0]])
